import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 63.4          # overall length (X)
W = 25.6          # overall depth  (Y)
H = 27.0          # overall height (Z)
WALL = 1.3        # side / back / end wall thickness
FRONT_WALL = 1.75 # front wall (carrying the studs)
FLOOR = 1.5       # floor thickness
MID_WALL = 1.75   # central partition thickness
RIB_T = 1.75      # rib thickness
RIB_L = 4.9       # rib length (from wall face)
EDGE_R = 0.35     # outer edge fillet

PITCH = 10.0      # stud pitch along X
N_COLS = 6
ROW_DZ = 7.7      # stud row offset from mid height
STUD_D = 4.5
STUD_LEN = 4.55
NOTCH_LEN = 0.75  # half-groove length along stud axis at the base
NOTCH_RI = 1.4    # half-groove inner radius

HOLE_D = 5.5      # central recess in the front face
HOLE_DEPTH = 0.8

# ---------------- body ----------------
body = (cq.Workplane("XY")
        .box(L, W, H, centered=(True, True, False))
        .edges().fillet(EDGE_R))

# two compartments
inner_L = (L - 2 * WALL - MID_WALL) / 2.0
inner_W = W - WALL - FRONT_WALL
inner_cy = -W / 2.0 + FRONT_WALL + inner_W / 2.0
for sx in (-1, 1):
    cx = sx * (MID_WALL / 2.0 + inner_L / 2.0)
    pocket = (cq.Workplane("XY")
              .box(inner_L, inner_W, H, centered=(True, True, False))
              .translate((cx, inner_cy, FLOOR)))
    body = body.cut(pocket)

# ribs on the cavity centre line (end walls and both sides of partition)
rib_h = H - FLOOR
rib_xs = [
    -L / 2 + WALL + RIB_L / 2,
    -MID_WALL / 2 - RIB_L / 2,
    MID_WALL / 2 + RIB_L / 2,
    L / 2 - WALL - RIB_L / 2,
]
for rx in rib_xs:
    rib = (cq.Workplane("XY")
           .box(RIB_L + 0.02, RIB_T, rib_h, centered=(True, True, False))
           .translate((rx, inner_cy, FLOOR - 0.01)))
    body = body.union(rib)

# ---------------- studs on the front (-Y) face ----------------
zc = H / 2.0
front_y = -W / 2.0


def make_stud():
    """Stud along -Y with its axis through the origin, base at y=0."""
    stud = cq.Workplane("XZ", origin=(0, 0.01, 0)).circle(STUD_D / 2.0).extrude(STUD_LEN + 0.01)
    # put the cylinder seam at the back (-X side)
    stud = stud.rotate((0, 0, 0), (0, 1, 0), 180)
    # half-ring groove on the underside of the stud, at the base
    ring = (cq.Workplane("XZ", origin=(0, 0.02, 0))
            .circle(STUD_D / 2.0 + 0.5).circle(NOTCH_RI)
            .extrude(NOTCH_LEN + 0.02))
    lower = (cq.Workplane("XY")
             .box(STUD_D + 2, NOTCH_LEN + 0.04, STUD_D / 2.0 + 1,
                  centered=(True, False, False))
             .translate((0, -NOTCH_LEN, -STUD_D / 2.0 - 1)))
    return stud.cut(ring.intersect(lower))


stud0 = make_stud()
for row in (-1, 1):
    z = zc + row * ROW_DZ
    for i in range(N_COLS):
        x = (i - (N_COLS - 1) / 2.0) * PITCH
        body = body.union(stud0.translate((x, front_y, z)))

# central shallow recess
hole = (cq.Workplane("XZ", origin=(0, front_y - 0.01, 0))
        .center(0, zc).circle(HOLE_D / 2.0).extrude(-(HOLE_DEPTH + 0.01)))
body = body.cut(hole)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
